import math
import cadquery as cq

# ---------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------
# Clip body: flange plate + meander spring + two fingers
L_FL = 80.0          # flange length (X)
XC = L_FL / 2.0      # symmetry plane of the clip
H = 16.0             # height of flange / meander / fingers
FL_Y0 = 47.8         # flange front face
FL_T = 2.1           # flange thickness
FL_CH = 4.2          # 45 deg chamfer on flange ends
END_HOLE_D = 4.4
END_HOLE_X = 5.6     # from each end
END_HOLE_Z = 8.0
LUG_R = 5.2
LUG_Z = 21.2         # lug hole centre height
LUG_HOLE_D = 4.6
LUG_FIL = 5.0

# meander spring
W = 2.1              # strip width
S = 0.5              # slot width
RO = W + S / 2.0     # outer bend radius
Y_BOT = 38.3         # meander front edge
Y_TOP = 45.7         # meander back edge
YL = Y_BOT + RO      # lower arc centres
YU = Y_TOP - RO      # upper arc centres
STEM_X = 28.2        # end stems distance from symmetry plane
STEM_YS = 45.5       # start of the S bend
STEM_R = 1.6         # centre-line radius of the S bend

# slot positions (relative to XC, left half; mirrored)
T_SLOTS = [-24.8, -19.4, -7.85]         # open towards flange
T_SLOTS_FULL = [-2.55]                  # open up to the flange
B_SLOTS = [-22.0, -16.35, -11.05, -5.2]  # open towards front
# U bends (bottom caps) and top caps  (x ranges, left half)
U_CAPS = [(-27.15, -22.25), (-21.75, -16.6), (-10.8, -5.45), (-4.95, -0.25)]
TOP_CAPS = [(-24.55, -19.65), (-19.15, -8.1), (-7.6, -2.8)]
MID_HALF = 2.3

# fingers (right finger given, left one mirrored)
F_IN = 11.3          # inner face distance from XC
F_OUT = 16.1         # outer face distance from XC
F_R1 = 5.15          # bulb main lobe radius
F_Y1 = 16.7          # bulb lobe centre Y
F_R2 = 3.0           # tip radius
F_Y2 = 8.8           # tip centre Y (front end = F_Y2 - F_R2)
F_FLANK_R = 15.0     # radius of the convex flank between lobe and tip

# Column block (separate body)
C_XL = 0.3
C_XR = 23.2
C_XM = (C_XL + C_XR) / 2.0
C_H = 42.5           # tall column height
C_STEP_H = 21.5      # step height
C_BACK = 37.7        # back face of step
C_YC = 13.4          # centre line of the front corner rounds
C_CORNER = 3.2       # front corner radius
CHIN_R = 6.1         # chin radius (chin front at Y=0)
CHIN_FIL = 4.8       # concave blend chin / body
ARC_SIDE_Y = 18.8    # where the back rounds of the tall part meet the sides
ARC_TOP_Y = 27.25    # back face of the tall part
SLOPE_C = 21.5       # 45 deg under-cut plane  Y + Z = SLOPE_C
BASE_H = 6.5         # foot plate height
BASE_Y0 = SLOPE_C - BASE_H
BASE_R = 4.5
HOLE1_Y = 20.75
HOLE2_Y = 32.5
CB_D = 9.6
THRU_D = 5.2
CB_FLOOR = 8.0


Q45 = math.cos(math.pi / 4)

# ---------------------------------------------------------------
# helpers
# ---------------------------------------------------------------
def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl(cx, cy, r, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0).center(cx, cy)
            .circle(r).extrude(z1 - z0))


def cap(a, b, y0, y1, r, top=True, z1=H):
    """rectangle x[a,b] y[y0,y1] with the two corners on the top (or bottom)
    side rounded with radius r (a full half-round if the width is 2r)"""
    half = (b - a) / 2.0
    full = r >= half - 1e-6
    r = min(r, half)
    q = Q45
    wp = cq.Workplane("XY")
    if top:
        wp = wp.moveTo(a, y0).lineTo(b, y0).lineTo(b, y1 - r)
        if full:
            wp = wp.threePointArc((a + half, y1), (a, y1 - r))
        else:
            wp = (wp.threePointArc((b - r + r * q, y1 - r + r * q), (b - r, y1))
                  .lineTo(a + r, y1)
                  .threePointArc((a + r - r * q, y1 - r + r * q), (a, y1 - r)))
    else:
        wp = wp.moveTo(a, y1).lineTo(a, y0 + r)
        if full:
            wp = wp.threePointArc((a + half, y0), (b, y0 + r))
        else:
            wp = (wp.threePointArc((a + r - r * q, y0 + r - r * q), (a + r, y0))
                  .lineTo(b - r, y0)
                  .threePointArc((b - r + r * q, y0 + r - r * q), (b, y0 + r)))
        wp = wp.lineTo(b, y1)
    return wp.close().extrude(z1)


def slot(x, y_closed, y_open, s=S):
    """straight slot of width s, rounded at y_closed, running to y_open"""
    r = s / 2.0
    lo, hi = min(y_closed, y_open), max(y_closed, y_open)
    b = box(x - r, x + r, lo, hi, -1, H + 1)
    return b.union(cyl(x, y_closed, r, -1, H + 1))


# ---------------------------------------------------------------
# meander spring (left half built in relative X, then mirrored)
# ---------------------------------------------------------------
def meander_half():
    parts = []
    # centre band
    parts.append(box(U_CAPS[0][0], 0.0, YL, YU, 0, H))
    for a, b in U_CAPS:
        parts.append(cap(a, b, Y_BOT, YU, RO, top=False))
    for a, b in TOP_CAPS:
        parts.append(cap(a, b, YL, Y_TOP, RO, top=True))
    # middle stem up into the flange
    parts.append(box(-MID_HALF, 0.0, YL, FL_Y0 + 0.3, 0, H))
    # S shaped end stem from the flange into the first leg: two tangent
    # bends of centre-line radius STEM_R, jog = leg pitch
    x0 = -STEM_X
    r = STEM_R
    jog = W
    th = math.acos(1.0 - jog / (2.0 * r))
    ys = STEM_YS
    c1 = (x0 + r, ys)
    u = (-math.cos(th), -math.sin(th))
    c2 = (c1[0] + 2 * r * u[0], c1[1] + 2 * r * u[1])
    ro, ri = r + W / 2.0, r - W / 2.0

    def pt(c, rad, ang):
        return (c[0] + rad * math.cos(ang), c[1] + rad * math.sin(ang))

    a180 = math.pi
    s_bend = (cq.Workplane("XY")
              .moveTo(x0 - W / 2, FL_Y0 + 0.3)
              .lineTo(x0 - W / 2, ys)
              .threePointArc(pt(c1, ro, a180 + th / 2), pt(c1, ro, a180 + th))
              .threePointArc(pt(c2, ri, th / 2), pt(c2, ri, 0.0))
              .lineTo(c2[0] + ri, YL)
              .lineTo(c2[0] + ro, YL)
              .lineTo(c2[0] + ro, c2[1])
              .threePointArc(pt(c2, ro, th / 2), pt(c2, ro, th))
              .threePointArc(pt(c1, ri, a180 + th / 2), pt(c1, ri, a180))
              .lineTo(x0 + W / 2, FL_Y0 + 0.3)
              .close().extrude(H))
    parts.append(s_bend)
    res = parts[0]
    for p in parts[1:]:
        res = res.union(p)
    return res


def _circle_intersection(c1, r1, c2, r2, key):
    dx, dy = c2[0] - c1[0], c2[1] - c1[1]
    d = math.hypot(dx, dy)
    a = (d * d + r1 * r1 - r2 * r2) / (2 * d)
    h = math.sqrt(max(r1 * r1 - a * a, 0.0))
    bx, by = c1[0] + a * dx / d, c1[1] + a * dy / d
    sols = [(bx - h * dy / d, by + h * dx / d), (bx + h * dy / d, by - h * dx / d)]
    return max(sols, key=key)


def _arc_mid(c, r, p0, p1, ccw=True):
    a0 = math.atan2(p0[1] - c[1], p0[0] - c[0])
    a1 = math.atan2(p1[1] - c[1], p1[0] - c[0])
    if ccw:
        while a1 <= a0:
            a1 += 2 * math.pi
    else:
        while a1 >= a0:
            a1 -= 2 * math.pi
    am = (a0 + a1) / 2.0
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


def finger_right():
    """right finger (relative X), bulb pointing towards the centre.
    Bulb outline: lobe arc + large convex flank arc + tip arc (all tangent)."""
    c1 = (F_OUT - F_R1, F_Y1)
    c2 = (F_OUT - F_R2, F_Y2)
    rb = F_FLANK_R
    q = _circle_intersection(c1, rb - F_R1, c2, rb - F_R2, key=lambda p: p[0])
    t1 = (q[0] + rb * (c1[0] - q[0]) / (rb - F_R1),
          q[1] + rb * (c1[1] - q[1]) / (rb - F_R1))
    t2 = (q[0] + rb * (c2[0] - q[0]) / (rb - F_R2),
          q[1] + rb * (c2[1] - q[1]) / (rb - F_R2))
    yj = c1[1] + math.sqrt(F_R1 ** 2 - (F_IN - c1[0]) ** 2)
    pj = (F_IN, yj)
    pe = (F_OUT, c2[1])
    wp = (cq.Workplane("XY")
          .moveTo(F_OUT, YU)
          .lineTo(F_IN, YU)
          .lineTo(*pj)
          .threePointArc(_arc_mid(c1, F_R1, pj, t1, True), t1)
          .threePointArc(_arc_mid(q, rb, t1, t2, True), t2)
          .threePointArc(_arc_mid(c2, F_R2, t2, pe, True), pe)
          .close())
    return wp.extrude(H)


def clip_body():
    half = meander_half().union(finger_right().mirror("YZ"))
    full = half.union(half.mirror("YZ"))
    # cut slots
    for xs in T_SLOTS:
        for sg in (-1, 1):
            full = full.cut(slot(sg * xs, YL, Y_TOP + 1.0))
    for xs in T_SLOTS_FULL:
        for sg in (-1, 1):
            full = full.cut(slot(sg * xs, YL, FL_Y0))
    for xs in B_SLOTS:
        for sg in (-1, 1):
            full = full.cut(slot(sg * xs, YU, Y_BOT - 1.0))
    full = full.cut(slot(0.0, YU, Y_BOT - 1.0))
    full = full.translate((XC, 0, 0))

    # flange plate with chamfered ends and lug
    lx0, lx1 = XC - LUG_R, XC + LUG_R
    prof = (cq.Workplane("XZ")
            .moveTo(0, FL_CH).lineTo(FL_CH, 0).lineTo(L_FL - FL_CH, 0)
            .lineTo(L_FL, FL_CH).lineTo(L_FL, H - FL_CH)
            .lineTo(L_FL - FL_CH, H)
            .lineTo(lx1 + LUG_FIL, H)
            .threePointArc((lx1 + LUG_FIL - LUG_FIL * Q45, H + LUG_FIL - LUG_FIL * Q45),
                           (lx1, H + LUG_FIL))
            .lineTo(lx1, LUG_Z)
            .threePointArc((XC, LUG_Z + LUG_R), (lx0, LUG_Z))
            .lineTo(lx0, H + LUG_FIL)
            .threePointArc((lx0 - LUG_FIL + LUG_FIL * Q45, H + LUG_FIL - LUG_FIL * Q45),
                           (lx0 - LUG_FIL, H))
            .lineTo(FL_CH, H).lineTo(0, H - FL_CH).close()
            .extrude(-FL_T)
            .translate((0, FL_Y0, 0)))
    # holes through the flange (along Y)
    for hx, hz, hd in ((END_HOLE_X, END_HOLE_Z, END_HOLE_D),
                       (L_FL - END_HOLE_X, END_HOLE_Z, END_HOLE_D),
                       (XC, LUG_Z, LUG_HOLE_D)):
        hole = (cq.Workplane("XZ").workplane(offset=-(FL_Y0 - 1))
                .center(hx, hz).circle(hd / 2.0).extrude(-(FL_T + 2)))
        prof = prof.cut(hole)
    return full.union(prof)


# ---------------------------------------------------------------
# column block
# ---------------------------------------------------------------
def column_body():
    xl, xr, xm = C_XL, C_XR, C_XM
    q = math.cos(math.pi / 4)
    # front outline: two big corner arcs blended into the round chin with
    # concave fillets (all tangent)
    rc, rch, rf = C_CORNER, CHIN_R, CHIN_FIL
    cl = (xl + rc, C_YC)
    cc = (xm, rch)
    r1, r2 = rc + rf, rch + rf
    dx, dy = cc[0] - cl[0], cc[1] - cl[1]
    d = math.hypot(dx, dy)
    a = (d * d + r1 * r1 - r2 * r2) / (2 * d)
    h = math.sqrt(r1 * r1 - a * a)
    bx, by = cl[0] + a * dx / d, cl[1] + a * dy / d
    p = (bx - h * dy / d, by + h * dx / d)
    if p[1] > by:
        p = (bx + h * dy / d, by - h * dx / d)
    ta = (cl[0] + rc * (p[0] - cl[0]) / r1, cl[1] + rc * (p[1] - cl[1]) / r1)
    tb = (cc[0] + rch * (p[0] - cc[0]) / r2, cc[1] + rch * (p[1] - cc[1]) / r2)

    def mx(pt):
        return (2 * xm - pt[0], pt[1])

    def mid_arc(c, r, p0, p1, ccw=True):
        a0 = math.atan2(p0[1] - c[1], p0[0] - c[0])
        a1 = math.atan2(p1[1] - c[1], p1[0] - c[0])
        if ccw:
            while a1 <= a0:
                a1 += 2 * math.pi
        else:
            while a1 >= a0:
                a1 -= 2 * math.pi
        am = (a0 + a1) / 2.0
        return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))

    cr = mx(cl)
    pr = mx(p)
    tar, tbr = mx(ta), mx(tb)
    rbk = ARC_TOP_Y - ARC_SIDE_Y     # big rounds of the tall part's back
    tall = (cq.Workplane("XY")
            .moveTo(xr, ARC_SIDE_Y)
            .threePointArc((xr - rbk + rbk * q, ARC_SIDE_Y + rbk * q),
                           (xr - rbk, ARC_TOP_Y))
            .lineTo(xl + rbk, ARC_TOP_Y)
            .threePointArc((xl + rbk - rbk * q, ARC_SIDE_Y + rbk * q),
                           (xl, ARC_SIDE_Y))
            .lineTo(xl, C_YC)
            .threePointArc(mid_arc(cl, rc, (xl, C_YC), ta, True), ta)
            .threePointArc(mid_arc(p, rf, ta, tb, False), tb)
            .threePointArc(mid_arc(cc, rch, tb, tbr, True), tbr)
            .threePointArc(mid_arc(pr, rf, tbr, tar, False), tar)
            .threePointArc(mid_arc(cr, rc, tar, (xr, C_YC), True), (xr, C_YC))
            .close()
            .extrude(C_H))
    rb = 3.5
    step = (cq.Workplane("XY")
            .moveTo(xl, BASE_Y0)
            .lineTo(xr, BASE_Y0)
            .lineTo(xr, C_BACK - rb)
            .threePointArc((xr - rb + rb * q, C_BACK - rb + rb * q), (xr - rb, C_BACK))
            .lineTo(xl + rb, C_BACK)
            .threePointArc((xl + rb - rb * q, C_BACK - rb + rb * q), (xl, C_BACK - rb))
            .close()
            .extrude(C_STEP_H))
    body = tall.union(step)
    # 45 degree under-cut at the front
    wedge = (cq.Workplane("YZ")
             .polyline([(-5, -5), (-5, SLOPE_C + 5), (SLOPE_C + 5, -5)]).close()
             .extrude(xr + 10).translate((-5, 0, 0)))
    body = body.cut(wedge)
    # foot plate under the slope
    rf = BASE_R
    foot = (cq.Workplane("XY")
            .moveTo(xl, C_BACK - rb)
            .lineTo(xl, BASE_Y0 + rf)
            .threePointArc((xl + rf - rf * q, BASE_Y0 + rf - rf * q), (xl + rf, BASE_Y0))
            .lineTo(xr - rf, BASE_Y0)
            .threePointArc((xr - rf + rf * q, BASE_Y0 + rf - rf * q), (xr, BASE_Y0 + rf))
            .lineTo(xr, C_BACK - rb)
            .threePointArc((xr - rb + rb * q, C_BACK - rb + rb * q), (xr - rb, C_BACK))
            .lineTo(xl + rb, C_BACK)
            .threePointArc((xl + rb - rb * q, C_BACK - rb + rb * q), (xl, C_BACK - rb))
            .close()
            .extrude(BASE_H))
    body = body.union(foot)

    # counterbored screw holes (drill point transition)
    def hole_tool(top):
        r1, r2 = THRU_D / 2.0, CB_D / 2.0
        cone_h = r2 - r1
        thru = cq.Workplane("XY").workplane(offset=-1).circle(r1).extrude(top + 2)
        cb = (cq.Workplane("XY").workplane(offset=CB_FLOOR)
              .circle(r2).extrude(top + 1 - CB_FLOOR))
        cone = cq.Workplane("XY").add(
            cq.Solid.makeCone(r1, r2, cone_h,
                              pnt=cq.Vector(0, 0, CB_FLOOR - cone_h)))
        return thru.union(cb).union(cone)

    body = body.cut(hole_tool(C_H).translate((xm, HOLE1_Y, 0)))
    body = body.cut(hole_tool(C_STEP_H).translate((xm, HOLE2_Y, 0)))
    return body


clip = clip_body()
column = column_body()

result = (cq.Workplane("XY")
          .add(cq.Compound.makeCompound([clip.val(), column.val()])))

VIEW = {"azimuth": 45, "elevation": 26}
